import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# pipe / drum axis is along X, Z up, part symmetric about XZ plane
PLATE_T = 10.0          # side plate thickness (X)
BODY_HX = 69.35         # half length of body in X (outer faces of side plates)
PLATE_HW = 74.0         # half width of side plates (Y)
FLANGE_R = 84.2         # radius of round lower part of side plates
TOP_PLATE_Z0 = 86.5     # underside of top plate (Z above axis)
TOP_PLATE_Z1 = 96.6     # top face of top plate

# +X side: raised ring + bore
RING_D = 118.5
RING_H = 4.4
BORE_D = 89.0
BORE_DEPTH = 14.0

# -X side: round boss with small centre hole
BOSS_D = 87.3
BOSS_H = 11.7
BOSS_HOLE_D = 15.5

# drum (attached to +X plate, free end towards -X)
DRUM1_D = 151.5         # large diameter next to +X plate
DRUM1_X0 = 11.35
DRUM2_D = 120.9         # small diameter end
DRUM2_X0 = -37.25

# top structure
STRIP_HW = 28.5         # half width of strip band (Y)
STRIP_Z1 = 106.6
WEB_HW = 10.0
WEB_Z1 = 126.7
PAD_HX = 28.8
PAD_Z1 = 113.0
RAIL_HL = 118.5
RAIL_HW = 6.75
RAIL_Z0 = 123.6
RAIL_Z1 = 140.2

# holes
STRIP_HOLE_D = 8.0
STRIP_HOLE_X = 52.5
STRIP_HOLE_Y = 19.3
RAIL_HOLE_D = 6.7
RAIL_HOLE_X = 43.8
BC_R = 71.0             # +X flange bolt circle
BOLT_D_SMALL = 5.3
BOLT_D_LARGE = 10.5
BOLT_DEPTH = 8.0
BC2_R = 67.0            # -X plate hole circle
BOLT2_D = 7.5
BC3_R = 36.5            # tapped holes on inner face of -X plate (behind boss)
BOLT3_D = 4.6
BOLT3_DEPTH = 10.0
PAD_HOLES = [(17.0, 34.0, 15.0), (13.0, 67.5, 6.0)]   # (x, y, d) from below
PAD_HOLE_DEPTH = 16.0


def side_plate(x0, x1):
    """D-shaped side plate: rectangle on top of a circle, in YZ plane."""
    t = x1 - x0
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    circ = wp.circle(FLANGE_R).extrude(t)
    rect = (cq.Workplane("YZ", origin=(x0, 0, 0))
            .center(0, TOP_PLATE_Z1 / 2.0)
            .rect(2 * PLATE_HW, TOP_PLATE_Z1)
            .extrude(t))
    return circ.union(rect)


def xwp(x0, seam=(0, 0, 1)):
    """Workplane normal to +X on the drum axis; `seam` sets where the
    cylinder seam edge lands (kept out of sight)."""
    return cq.Workplane(cq.Plane(origin=(x0, 0, 0), xDir=seam,
                                 normal=(1, 0, 0)))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# side plates
body = side_plate(-BODY_HX, -BODY_HX + PLATE_T)
body = body.union(side_plate(BODY_HX - PLATE_T, BODY_HX))

# top plate
body = body.union(box(-BODY_HX, BODY_HX, -PLATE_HW, PLATE_HW,
                      TOP_PLATE_Z0, TOP_PLATE_Z1))

# strips + web + pads
body = body.union(box(-BODY_HX, BODY_HX, -STRIP_HW, STRIP_HW,
                      TOP_PLATE_Z1 - 1, STRIP_Z1))
body = body.union(box(-BODY_HX, BODY_HX, -WEB_HW, WEB_HW,
                      TOP_PLATE_Z1 - 1, WEB_Z1))
for sgn in (-1, 1):
    y0, y1 = sorted((sgn * STRIP_HW, sgn * PLATE_HW))
    body = body.union(box(-PAD_HX, PAD_HX, y0, y1, TOP_PLATE_Z1 - 1, PAD_Z1))

# rail
body = body.union(box(-RAIL_HL, RAIL_HL, -RAIL_HW, RAIL_HW, RAIL_Z0, RAIL_Z1))

# drum
DRUM_SEAM = (0, math.sin(math.radians(25)), math.cos(math.radians(25)))
drum1 = (xwp(DRUM1_X0, seam=DRUM_SEAM)
         .circle(DRUM1_D / 2).extrude(BODY_HX - PLATE_T - DRUM1_X0 + 1))
drum2 = (xwp(DRUM2_X0, seam=DRUM_SEAM)
         .circle(DRUM2_D / 2).extrude(DRUM1_X0 - DRUM2_X0 + 1))
body = body.union(drum1).union(drum2)

# +X raised ring
ring = (xwp(BODY_HX, seam=(0, 1, 0))
        .circle(RING_D / 2).extrude(RING_H))
body = body.union(ring)

# -X boss
boss = (xwp(-BODY_HX - BOSS_H, seam=(0, 0, -1))
        .circle(BOSS_D / 2).extrude(BOSS_H))
body = body.union(boss)

# bore in +X face (blind)
bore = (xwp(BODY_HX + RING_H - BORE_DEPTH, seam=(0, -1, 0))
        .circle(BORE_D / 2).extrude(BORE_DEPTH + 1))
body = body.cut(bore)

# centre hole in -X boss
chole = (xwp(-BODY_HX - BOSS_H - 1, seam=(0, -1, 0))
         .circle(BOSS_HOLE_D / 2).extrude(BOSS_H + PLATE_T + 2))
body = body.cut(chole)

# +X flange bolt holes (12 @ 30 deg, 3 larger at 90/210/330)
for i in range(12):
    a = math.radians(i * 30.0)
    y, z = BC_R * math.cos(a), BC_R * math.sin(a)
    large = (i * 30) % 360 in (90, 210, 330)
    d = BOLT_D_LARGE if large else BOLT_D_SMALL
    h = (cq.Workplane("YZ", origin=(BODY_HX - BOLT_DEPTH, y, z))
         .circle(d / 2).extrude(BOLT_DEPTH + 1))
    body = body.cut(h)

# -X plate through holes (6 @ 60 deg starting 30)
for i in range(6):
    a = math.radians(30.0 + i * 60.0)
    y, z = BC2_R * math.cos(a), BC2_R * math.sin(a)
    h = (cq.Workplane("YZ", origin=(-BODY_HX - 1, y, z))
         .circle(BOLT2_D / 2).extrude(PLATE_T + 2))
    body = body.cut(h)

# blind holes in the inner (+X) face of the -X plate (6 @ 60 deg from 0)
for i in range(6):
    a = math.radians(i * 60.0)
    y, z = BC3_R * math.cos(a), BC3_R * math.sin(a)
    h = (cq.Workplane("YZ", origin=(-BODY_HX + PLATE_T - BOLT3_DEPTH, y, z))
         .circle(BOLT3_D / 2).extrude(BOLT3_DEPTH + 1))
    body = body.cut(h)

# strip holes (through strip + top plate)
for sy in (-1, 1):
    for x in (-STRIP_HOLE_X, 0.0, STRIP_HOLE_X):
        h = (cq.Workplane("XY", origin=(x, sy * STRIP_HOLE_Y, TOP_PLATE_Z0 - 1))
             .circle(STRIP_HOLE_D / 2).extrude(STRIP_Z1 - TOP_PLATE_Z0 + 2))
        body = body.cut(h)

# blind holes from below into the pads
for sy in (-1, 1):
    for sx in (-1, 1):
        for (hx, hy, hd) in PAD_HOLES:
            h = (cq.Workplane("XY", origin=(sx * hx, sy * hy, TOP_PLATE_Z0 - 1))
                 .circle(hd / 2).extrude(PAD_HOLE_DEPTH + 1))
            body = body.cut(h)

# rail holes (through rail, web and top plate)
for x in (-RAIL_HOLE_X, 0.0, RAIL_HOLE_X):
    h = (cq.Workplane("XY", origin=(x, 0, TOP_PLATE_Z0 - 1))
         .circle(RAIL_HOLE_D / 2).extrude(RAIL_Z1 - TOP_PLATE_Z0 + 2))
    body = body.cut(h)

result = body
